# Slotted clip / detent holder: a tall front block with a through slot from the
# bottom, two thin side walls with a concave top arc, a 45deg slanted floor that
# is open at the back and top, and a spherical detent bump on each inner wall.
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
H = 60.0            # overall height (Z)
W = 20.4            # overall width (X), centred on X=0
D = 24.2            # overall depth (Y), front face at Y=0, open back at Y=D
T_FRONT = 4.75      # thickness of the front block (Y)
T_WALL = 2.4        # side wall thickness (X)
T_FLOOR = 4.0       # thickness of the slanted floor (normal to the underside)
ARC_R = 15.0        # concave arc on top of the side walls
Z_BACK_TOP = 45.45  # height of the side walls at the back
SLANT_Z0 = 21.46    # height where the (extended) underside plane meets the front plane
SLANT_ANG = 45.85   # underside angle from horizontal
R_FRONT_BOT = 11.0  # blend between front face and slanted underside
R_BACK_BOT = 2.4    # blend between underside and back edge
R_TOP_FRONT = 2.4   # top front edge round
R_INNER = 20.0      # inner blend between front block and floor
R_FLOOR_END = 1.9   # round on the back tip of the floor (inner side)
SLOT_W = 4.85       # slot width
SLOT_TOP = 48.0     # Z of the slot's rounded top (apex)
BUMP_R = 5.2        # detent bump sphere radius
BUMP_H = 3.75       # bump protrusion from the inner wall face
BUMP_Y = 14.9       # bump centre (Y)
BUMP_Z = 26.5       # bump centre (Z)

k = math.tan(math.radians(SLANT_ANG))          # slope of the underside


def slant_z(y, z0=SLANT_Z0):
    return z0 - k * y


# ---------------- outer body: side profile (YZ) extruded along X ----------------
# concave top arc: passes through (T_FRONT, H), horizontal tangent at Z_BACK_TOP
arc_cz = Z_BACK_TOP + ARC_R
arc_cy = T_FRONT + math.sqrt(ARC_R ** 2 - (H - arc_cz) ** 2)
a0 = math.atan2(H - arc_cz, T_FRONT - arc_cy)     # start angle
a1 = -math.pi / 2.0                              # end angle (bottom of circle)
am = 0.5 * (a0 + (a1 if a1 > a0 else a1 + 2 * math.pi))
arc_mid = (arc_cy + ARC_R * math.cos(am), arc_cz + ARC_R * math.sin(am))

profile = (
    cq.Workplane("YZ")
    .moveTo(0, SLANT_Z0)
    .lineTo(0, H)
    .lineTo(T_FRONT, H)
    .threePointArc(arc_mid, (arc_cy, Z_BACK_TOP))
    .lineTo(D, Z_BACK_TOP)
    .lineTo(D, slant_z(D))
    .close()
)
body = profile.extrude(W / 2.0, both=True)

# blends on the outer profile corners (edges parallel to X)
sel = cq.selectors.NearestToPointSelector
body = body.edges("|X").edges(sel((0, 0, SLANT_Z0))).fillet(R_FRONT_BOT)
body = body.edges("|X").edges(sel((0, D, slant_z(D)))).fillet(R_BACK_BOT)
body = body.edges("|X").edges(sel((0, 0, H))).fillet(R_TOP_FRONT)

# ---------------- pocket between the side walls (open top and back) ----------------
z_in0 = SLANT_Z0 + T_FLOOR * math.sqrt(1 + k * k)   # inner floor plane at Y=0
big = 40.0
pocket = (
    cq.Workplane("YZ")
    .moveTo(T_FRONT, z_in0 - k * T_FRONT)
    .lineTo(T_FRONT, H + big)
    .lineTo(D + big, H + big)
    .lineTo(D + big, z_in0 - k * (D + big))
    .close()
    .extrude((W - 2 * T_WALL) / 2.0, both=True)
)
pocket = pocket.edges("|X").edges(sel((0, T_FRONT, z_in0 - k * T_FRONT))).fillet(R_INNER)
body = body.cut(pocket)

# round the thin back tip of the floor (edge between floor and the back blend)
y_tip = D - 0.01
z_tip = z_in0 - k * y_tip
body = body.edges(sel((0, y_tip, z_tip))).fillet(R_FLOOR_END)

# ---------------- slot from the bottom, through the full depth ----------------
slot_len = SLOT_TOP + 20.0
slot = (
    cq.Workplane("XZ", origin=(0, -5, 0))
    .center(0, SLOT_TOP - slot_len / 2.0)
    .slot2D(slot_len, SLOT_W, angle=90)
    .extrude(-(D + 10))
)
body = body.cut(slot)

# ---------------- detent bumps on the inner faces of the side walls ----------------
for s in (-1, 1):
    xf = s * (W / 2.0 - T_WALL)                 # inner wall face
    xc = xf + s * (BUMP_R - BUMP_H)             # sphere centre (inside the wall)
    # sphere axis along Z; its seam meridian is turned to face into the wall
    sph_solid = cq.Solid.makeSphere(BUMP_R, cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), -90, 90, 360)
    if s < 0:
        sph_solid = sph_solid.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), 180)
    sph = cq.Workplane("XY").add(sph_solid.translate(cq.Vector(xc, BUMP_Y, BUMP_Z)))
    keep = (
        cq.Workplane("XY")
        .box(BUMP_H + 1.0, 4 * BUMP_R, 4 * BUMP_R)
        .translate((xf - s * (BUMP_H - 1.0) / 2.0, BUMP_Y, BUMP_Z))
    )
    body = body.union(sph.intersect(keep))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
